import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Truss-style mounting plate (lies in the XZ plane, thickness along Y)
# ---------------------------------------------------------------------------

# --- overall plate -----------------------------------------------------------
T = 6.0            # plate thickness (Y)
SIDE = 75.6        # half width of the plate body (X)
TOP = 28.7         # top edge height
BOT = 28.7         # bottom edge of the end sections (z = -BOT)
CB = 16.5          # bottom edge of the central section (z = -CB)

# --- corner ears -------------------------------------------------------------
EAR_X, EAR_Z, EAR_R = 71.6, 24.95, 6.8
EAR_HOLE_R = 2.0
EAR_FILLET = 0.6   # concave blend between ears and straight edges

# --- mounting holes ----------------------------------------------------------
HA_X, HA_Z, HA_R = 55.7, 22.1, 3.3      # upper hole (A)
HC_X, HC_Z, HC_R = 55.7, -22.1, 3.25    # lower hole (C) inside a lug
LUG_R = 6.6                              # lug around hole C (tangent to bottom)
HB_X, HB_Z, HB_R = 47.1, 17.3, 3.95     # inner hole (B)

# --- relief notch on the lower edge ------------------------------------------
NOTCH_X = 47.4
NOTCH_DZ = 0.4     # notch centre sits slightly below the central bottom edge
NOTCH_ROUND = 0.8

# --- truss cut-outs ----------------------------------------------------------
CUT_R = 1.6        # corner radius of the cut-outs
TIP_R = 0.9        # radius at the very acute tips of the end cut-outs
DIAG = 0.92        # slope dz/dx of the central diagonals
W1_LEFT, W1_TOP, W1_C = 37.5, 23.0, 27.4      # upper side windows
T_APEX, T_BOT = 18.9, -11.0                   # central triangle
# end cut-outs (left end, mirrored to the right)
TRI1 = [(-71.6, 18.2), (-71.6, -9.7), (-60.1, 18.2)]
TRI2_TOP = (-55.8, 13.4)
TRI2_BL = (-69.3, -18.1)
TRI2_BL_R = 2.4
BOSS_R = 6.7       # clearance ring kept around hole C


# ---------------------------------------------------------------------------
class Near(cq.Selector):
    """Select sketch vertices close to given 2D points."""

    def __init__(self, pts, tol=0.05):
        self.pts = pts
        self.tol = tol

    def filter(self, objs):
        out = []
        for o in objs:
            c = o.Center()
            if any(math.hypot(c.x - p[0], c.y - p[1]) < self.tol
                   for p in self.pts):
                out.append(o)
        return out


class OnCircle(cq.Selector):
    """Select sketch vertices lying on a given circle."""

    def __init__(self, c, r, tol=0.05):
        self.c, self.r, self.tol = c, r, tol

    def filter(self, objs):
        return [o for o in objs
                if abs(math.hypot(o.Center().x - self.c[0],
                                  o.Center().y - self.c[1]) - self.r)
                < self.tol]


def _unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def _pt(c, r, a):
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def _ang(c, p):
    return math.atan2(p[1] - c[1], p[0] - c[0])


def _short_mid(c, r, p0, p1):
    """Midpoint of the short arc of circle (c, r) between p0 and p1."""
    a0, a1 = _ang(c, p0), _ang(c, p1)
    d = (a1 - a0 + math.pi) % (2 * math.pi) - math.pi
    return _pt(c, r, a0 + d / 2)


# ---------------------------------------------------------------------------
# Outer outline (left half computed, right half mirrored)
# segments: ("L", start, end) or ("A", start, mid, end)
# ---------------------------------------------------------------------------
def left_half_segments():
    segs = []
    E_top = (-EAR_X, EAR_Z)
    E_bot = (-EAR_X, -EAR_Z)
    rf = EAR_FILLET
    re = EAR_R

    # -- top edge / upper ear concave blend (centre above the top line)
    fz = TOP + rf
    fx = E_top[0] + math.sqrt((re + rf) ** 2 - (fz - E_top[1]) ** 2)
    F1 = (fx, fz)
    A = (fx, TOP)
    u = _unit((F1[0] - E_top[0], F1[1] - E_top[1]))
    P1 = (E_top[0] + re * u[0], E_top[1] + re * u[1])
    segs.append(("A", A, _short_mid(F1, rf, A, P1), P1))

    # -- ear arc (long way round the outside) and side blend
    gx = -SIDE - rf
    gz = E_top[1] - math.sqrt((re + rf) ** 2 - (gx - E_top[0]) ** 2)
    G1 = (gx, gz)
    u = _unit((G1[0] - E_top[0], G1[1] - E_top[1]))
    P2 = (E_top[0] + re * u[0], E_top[1] + re * u[1])
    b0, b1 = _ang(E_top, P1), _ang(E_top, P2)
    if b1 < b0:
        b1 += 2 * math.pi
    segs.append(("A", P1, _pt(E_top, re, 0.5 * (b0 + b1)), P2))
    Q2 = (-SIDE, gz)
    segs.append(("A", P2, _short_mid(G1, rf, P2, Q2), Q2))

    # -- straight side, then lower ear (mirror of upper ear in z)
    Q3 = (-SIDE, -gz)
    segs.append(("L", Q2, Q3))
    G2 = (gx, -gz)
    P3 = (P2[0], -P2[1])
    segs.append(("A", Q3, _short_mid(G2, rf, Q3, P3), P3))
    P4 = (P1[0], -P1[1])
    segs.append(("A", P3, _pt(E_bot, re, -0.5 * (b0 + b1)), P4))
    F2 = (fx, -fz)
    A2 = (fx, -BOT)
    segs.append(("A", P4, _short_mid(F2, rf, P4, A2), A2))

    # -- bottom edge to the lug (lug is tangent to the bottom edge)
    L = (-HC_X, HC_Z)
    rl = LUG_R
    Lb = (L[0], L[1] - rl)
    segs.append(("L", A2, Lb))

    # -- lug arc up to the tangency with the relief notch
    N = (-NOTCH_X, -CB - NOTCH_DZ)
    dn = math.hypot(N[0] - L[0], N[1] - L[1])
    rn = dn - rl
    th = _ang(L, N)
    Tp = _pt(L, rl, th)
    segs.append(("A", Lb, _pt(L, rl, 0.5 * (-math.pi / 2 + th)), Tp))

    # -- notch arc (concave) over the top, ending in a small convex round
    rs = NOTCH_ROUND
    sz = -CB + rs
    sx = N[0] + math.sqrt((rn + rs) ** 2 - (sz - N[1]) ** 2)
    S = (sx, sz)
    u = _unit((S[0] - N[0], S[1] - N[1]))
    Np = (N[0] + rn * u[0], N[1] + rn * u[1])
    n0 = th + math.pi
    n1 = _ang(N, Np)
    segs.append(("A", Tp, _pt(N, rn, 0.5 * (n0 + n1)), Np))
    B = (sx, -CB)
    segs.append(("A", Np, _short_mid(S, rs, Np, B), B))
    return A, B, segs


def outline_wire():
    A, B, segs = left_half_segments()

    def mir(p):
        return (-p[0], p[1])

    right = []
    for s in reversed(segs):
        if s[0] == "L":
            right.append(("L", mir(s[2]), mir(s[1])))
        else:
            right.append(("A", mir(s[3]), mir(s[2]), mir(s[1])))
    allsegs = segs + [("L", B, mir(B))] + right + [("L", mir(A), A)]
    w = cq.Workplane("XZ", origin=(0, T / 2, 0)).moveTo(*A)
    for s in allsegs[:-1]:
        if s[0] == "L":
            w = w.lineTo(*s[2])
        else:
            w = w.threePointArc(s[2], s[3])
    return w.close()


# XZ workplane normal is -Y: start at y=+T/2 and extrude T towards -Y
plate = outline_wire().extrude(T)


def tool_from_sketch(sk):
    """Through-cut prism from a 2D sketch (single-direction extrusion)."""
    return (cq.Workplane("XZ", origin=(0, T, 0))
            .placeSketch(sk).extrude(2 * T))


def mirror_pts(pts):
    return [(-x, z) for (x, z) in pts]


def poly_sketch(pts, radii):
    sk = cq.Sketch().polygon(list(pts) + [pts[0]])
    for p, r in zip(pts, radii):
        sk = sk.vertices(Near([p], 0.05)).fillet(r).reset()
    return sk


# --- holes -------------------------------------------------------------------
hole_sk = cq.Sketch()
for (x, z, r) in [(EAR_X, EAR_Z, EAR_HOLE_R), (EAR_X, -EAR_Z, EAR_HOLE_R),
                  (HA_X, HA_Z, HA_R), (HC_X, HC_Z, HC_R), (HB_X, HB_Z, HB_R)]:
    hole_sk = hole_sk.push([(x, z), (-x, z)]).circle(r).reset()
plate = plate.cut(tool_from_sketch(hole_sk))

# --- central truss windows ---------------------------------------------------
w1_tr = ((W1_TOP - W1_C) / DIAG, W1_TOP)
w1_bl = (-W1_LEFT, W1_C - DIAG * W1_LEFT)
W1 = [(-W1_LEFT, W1_TOP), w1_bl, w1_tr]
t_bx = (T_BOT - T_APEX) / DIAG
TRI_C = [(0.0, T_APEX), (t_bx, T_BOT), (-t_bx, T_BOT)]

plate = plate.cut(tool_from_sketch(poly_sketch(W1, [CUT_R] * 3)))
plate = plate.cut(tool_from_sketch(poly_sketch(mirror_pts(W1), [CUT_R] * 3)))
plate = plate.cut(tool_from_sketch(poly_sketch(TRI_C, [CUT_R] * 3)))

# --- end cut-outs ------------------------------------------------------------
tri1_r = [CUT_R, TIP_R, CUT_R]
plate = plate.cut(tool_from_sketch(poly_sketch(TRI1, tri1_r)))
plate = plate.cut(tool_from_sketch(poly_sketch(mirror_pts(TRI1), tri1_r)))


def tri2_sketch(sign):
    top = (sign * TRI2_TOP[0], TRI2_TOP[1])
    bl = (sign * TRI2_BL[0], TRI2_BL[1])
    br = (sign * TRI2_TOP[0], TRI2_BL[1])
    boss = (sign * -HC_X, HC_Z)
    sk = cq.Sketch().polygon([top, bl, br, top])
    sk = sk.push([boss]).circle(BOSS_R, mode="s").reset()
    sk = sk.vertices(Near([top], 0.05)).fillet(TIP_R).reset()
    sk = sk.vertices(Near([bl], 0.05)).fillet(TRI2_BL_R).reset()
    sk = sk.vertices(OnCircle(boss, BOSS_R, 0.05)).fillet(0.8).reset()
    return sk


plate = plate.cut(tool_from_sketch(tri2_sketch(1)))
plate = plate.cut(tool_from_sketch(tri2_sketch(-1)))

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
